import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 75.0          # outer radius of the hemispherical shell
T = 3.6           # shell wall thickness (flat annular rim on the front plane)
STEM_W = 9.6      # square stem cross-section (X and Y)
STEM_L = 68.0     # stem length below the bottom of the shell

RI = R - T        # inner (cavity) radius
# The spheres' polar axis (and seam) is kept in the rim plane Y=0 and turned about Y by
# POLE_ANGLE; this only affects how the exact sphere is parametrised, not the shape.
POLE_ANGLE_OUTER = 0.0
POLE_ANGLE_INNER = -34.5


def sphere(r, pole_angle):
    return cq.Workplane("XY").sphere(r).rotate((0, 0, 0), (0, 1, 0), pole_angle)


def half_space(sign):
    """big box covering Y>0 (sign=+1) or Y<0 (sign=-1)"""
    return cq.Workplane("XY").box(4 * R, 2 * R, 4 * R).translate((0, sign * R, 0))


# Solid half sphere: flat face on the plane Y=0 (front), dome bulging toward +Y
dome = sphere(R, POLE_ANGLE_OUTER).intersect(half_space(+1))

# Square stem hanging straight down from the bottom of the shell; its front face is
# flush with the rim plane (Y=0) and its top is buried in the shell wall.
stem_top = -(R - T / 2.0)
stem_bot = -(R + STEM_L)
stem = (
    cq.Workplane("XY")
    .box(STEM_W, STEM_W, stem_top - stem_bot, centered=(True, False, False))
    .translate((0, 0, stem_bot))
)

body = dome.union(stem)

# Hollow the bowl: remove the inner half sphere, leaving a wall of thickness T
# (the body has no material at Y<0, so the whole inner sphere can be subtracted)
result = body.cut(sphere(RI, POLE_ANGLE_INNER))

VIEW = {"azimuth": 45, "elevation": 26}
